import cadquery as cq
import math

# ---------------------------------------------------------------
# Small sensor breakout PCB (0.9" x 1.0") with two JST-SH 4-pin
# side-entry connectors, a leadless IC, TSSOP-16, SOT-23-5, SC70-6,
# three 4x0603 resistor arrays and passives.  Units: mm.
# Board bottom at z=0, component side (top) at z=BOARD_T.
# ---------------------------------------------------------------

BOARD_W = 22.86          # X
BOARD_L = 25.40          # Y
BOARD_T = 1.60           # thickness
CORNER_R = 2.54          # plan corner radius

MOUNT_HOLE_D = 2.50
MOUNT_X = BOARD_W / 2 - 2.54
MOUNT_Y = BOARD_L / 2 - 2.54

PIN_HOLE_D = 1.00
PIN_PITCH = 2.54
PIN_COL_X = BOARD_W / 2 - 2.54
PIN_COUNT = 6

VIA_D = 0.45

# JST-SH 4 pin side entry connector
CON_W = 6.10
CON_D = 4.32
CON_H = 2.92
CON_INSET = 0.26         # gap between board edge and connector face
CON_PITCH = 1.00

T = BOARD_T


# ---------------------------------------------------------------
# helpers
# ---------------------------------------------------------------
def box(x0, x1, y0, y1, z0, z1):
    x0, x1 = min(x0, x1), max(x0, x1)
    y0, y1 = min(y0, y1), max(y0, y1)
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def fuse_all(base, parts):
    """Fuse several Workplane solids into base with a single boolean."""
    shp = base.val().fuse(*[p.val() for p in parts]).clean()
    return cq.Workplane("XY").newObject([shp])


def rbox(cx, cy, sx, sy, h, r=0.1, z0=T):
    """Box sitting on the board with filleted edges (capacitor-like)."""
    b = cq.Workplane("XY").box(sx, sy, h).translate((cx, cy, z0 + h / 2))
    if r > 0:
        b = b.edges("|Z").fillet(r).faces(">Z").edges().fillet(r * 0.9)
    return b


# ---------------------------------------------------------------
# board
# ---------------------------------------------------------------
board = (cq.Workplane("XY")
         .rect(BOARD_W, BOARD_L)
         .extrude(BOARD_T)
         .edges("|Z").fillet(CORNER_R))

mount_pts = [(sx * MOUNT_X, sy * MOUNT_Y) for sx in (-1, 1) for sy in (-1, 1)]
board = board.faces(">Z").workplane().pushPoints(mount_pts).hole(MOUNT_HOLE_D)

pin_pts = []
for sx in (-1, 1):
    for i in range(PIN_COUNT):
        y = (i - (PIN_COUNT - 1) / 2) * PIN_PITCH
        pin_pts.append((sx * PIN_COL_X, y))
board = board.faces(">Z").workplane().pushPoints(pin_pts).hole(PIN_HOLE_D)

via_pts = [
    # visible from the component side
    (-4.60, 10.27), (2.47, 6.11), (6.69, 6.35), (-3.51, 3.26),
    (-5.17, 2.68), (-2.54, -3.20), (0.09, -3.96), (-9.82, -5.12),
    (-6.08, -10.15), (-4.05, -9.36), (6.22, -11.72),
    # hidden under components, visible from below
    (0.28, -9.45), (1.59, -9.35), (3.76, -6.75), (-2.62, -8.05),
    (2.26, -2.08), (4.28, -2.12), (5.97, -1.50), (3.95, -1.04),
    (5.02, 1.00), (6.18, 1.08), (3.43, 1.04),
    (-4.70, 8.05), (-2.51, 9.15), (-1.24, 9.12), (0.50, 9.23),
    (1.93, 9.05), (0.04, 11.38),
]
board = board.faces(">Z").workplane().pushPoints(via_pts).hole(VIA_D)


# ---------------------------------------------------------------
# JST-SH connector, built with opening facing -Y, front face at y=0
# ---------------------------------------------------------------
def jst_sh():
    w2 = CON_W / 2
    d_main = 3.77                      # roof depth
    h_rear = 2.45                      # rear contact carrier height
    body = box(-w2, w2, 0, d_main, 0, CON_H)
    # chamfer the long top edges of the roof
    body = body.faces(">Z").edges("|Y").chamfer(0.22)
    # rear contact carrier: one rib per contact, recessed in between
    rear = box(-w2, w2, d_main - 0.01, CON_D, 0, h_rear)
    for i in range(5):
        x = (i - 2) * CON_PITCH
        rear = rear.cut(box(x - 0.22, x + 0.22, d_main + 0.15, CON_D + 0.1, -0.1, h_rear + 0.1))
    body = body.union(rear)
    # receptacle cavity
    cav_w = 4.75
    body = body.cut(box(-cav_w / 2, cav_w / 2, -0.1, 3.35, 0.32, 2.62))
    # thin front frame around the opening
    body = body.cut(box(-cav_w / 2 - 0.18, cav_w / 2 + 0.18, -0.1, 0.22, 0.20, 2.72))
    # keyed contact tongue hanging from the roof of the cavity
    tongue = (cq.Workplane("XZ")
              .polyline([(-cav_w / 2, 2.63), (-cav_w / 2, 2.48), (-1.52, 1.57),
                         (0.48, 1.57), (cav_w / 2, 2.52), (cav_w / 2, 2.63)])
              .close().extrude(-(3.35 - 0.95))
              .translate((0, 0.95, 0)))
    body = body.union(tongue)
    # contact slots in the tongue face / contact showing under the key slope
    for i in range(4):
        x = (i - 1.5) * CON_PITCH
        slot = (cq.Workplane("XZ").center(x, 1.82).slot2D(0.50, 0.24, angle=90)
                .extrude(-0.45).translate((0, 0.9, 0)))
        if i < 3:
            body = body.cut(slot)
        else:
            body = body.union(slot.translate((0, 0.45, 0)))
    # guide rails inside the cavity
    for s in (-1, 1):
        body = body.union(box(s * cav_w / 2, s * (cav_w / 2 - 0.25), 0.2, 3.35, 1.30, 1.48))
    for s in (-1, 1):
        # side slot for the metal hold-down
        body = body.cut(box(s * (w2 + 0.1), s * (w2 - 0.38), -0.1, 1.45, -0.1, 1.10))
        # hold-down tab
        body = body.union(box(s * (w2 - 0.06), s * (w2 - 0.26), 0.12, 1.35, 0.0, 0.95))
        # step in the side wall at the top rear (with a sloped front end)
        step = (cq.Workplane("YZ")
                .polyline([(2.70, CON_H + 0.1), (2.70, CON_H + 0.05), (3.05, CON_H - 0.42),
                           (d_main + 0.1, CON_H - 0.42), (d_main + 0.1, CON_H + 0.1)])
                .close().extrude(0.45)
                .translate((w2 - 0.45, 0, 0)))
        if s < 0:
            step = step.mirror("YZ")
        body = body.cut(step)
        # rear corner blocks lower than the carrier
        body = body.cut(box(s * (w2 + 0.1), s * (w2 - 0.5), d_main + 0.3, CON_D + 0.1,
                            h_rear - 0.6, h_rear + 0.1))
    # rear pins: vertical strip on each rib, joggled out into an SMD foot
    pin_prof = [(CON_D - 0.05, h_rear - 0.22), (CON_D + 0.08, h_rear - 0.22),
                (CON_D + 0.08, 0.42), (CON_D + 0.36, 0.15), (CON_D + 0.80, 0.15),
                (CON_D + 0.80, 0.0), (CON_D + 0.30, 0.0), (CON_D - 0.05, 0.34)]
    pins = []
    for i in range(4):
        x = (i - 1.5) * CON_PITCH
        pins.append(cq.Workplane("YZ").polyline(pin_prof).close()
                    .extrude(0.15, both=True).translate((x, 0, 0)))
    return fuse_all(body, pins)


def place_con(shape, front_y, facing):
    """facing = -1 -> opening to -Y at y=front_y, +1 -> opening to +Y."""
    if facing < 0:
        return shape.translate((0, front_y, T))
    return shape.rotate((0, 0, 0), (0, 0, 1), 180).translate((0, front_y, T))


con = jst_sh()
j_front = place_con(con, -BOARD_L / 2 + CON_INSET, -1)
j_back = place_con(con, BOARD_L / 2 - CON_INSET, 1)


# ---------------------------------------------------------------
# ICs
# ---------------------------------------------------------------
def gullwing(length, width, h_body, foot=0.38, t=0.12, bend_r=0.22, theta_deg=65.0, exit_frac=0.48):
    """Gull-wing lead with radiused bends.  Profile in YZ (outward = +Y),
    extruded symmetrically along X."""
    th = math.radians(theta_deg)
    zc = h_body * exit_frac + t / 2     # centre line of the upper leg
    zf = t / 2                          # centre line of the foot
    R = bend_r
    s = (zc - zf - 2 * R * (1 - math.cos(th))) / math.sin(th)
    # horizontal position of the first bend chosen so the foot has `foot` length
    y1 = length - foot - 2 * R * math.sin(th) - s * math.cos(th)
    c1 = (y1, zc - R)
    e1 = (y1 + R * math.sin(th), zc - R + R * math.cos(th))
    s2 = (e1[0] + s * math.cos(th), e1[1] - s * math.sin(th))
    c2 = (s2[0] + R * math.sin(th), s2[1] + R * math.cos(th))
    h = t / 2

    def arc_pt(c, r, ang):        # ang measured from +Z axis toward +Y
        return (c[0] + r * math.sin(ang), c[1] + r * math.cos(ang))

    def arc2_pt(c, r, ang):       # ang measured from -Z axis toward -Y
        return (c[0] - r * math.sin(ang), c[1] - r * math.cos(ang))

    ro, ri = R + h, R - h
    wp = (cq.Workplane("YZ")
          .moveTo(-0.05, zc + h)
          .lineTo(y1, zc + h)
          .threePointArc(arc_pt(c1, ro, th / 2), arc_pt(c1, ro, th))
          .lineTo(*arc2_pt(c2, ri, th))
          .threePointArc(arc2_pt(c2, ri, th / 2), (c2[0], c2[1] - ri))
          .lineTo(length, zf + h)
          .lineTo(length, 0.0)
          .lineTo(c2[0], 0.0)
          .threePointArc(arc2_pt(c2, ro, th / 2), arc2_pt(c2, ro, th))
          .lineTo(*arc_pt(c1, ri, th))
          .threePointArc(arc_pt(c1, ri, th / 2), (y1, zc - h))
          .lineTo(-0.05, zc - h)
          .close())
    return wp.extrude(width / 2, both=True)


def ic_body(sx, sy, h, draft=0.12):
    """Moulded body: straight lower half, tapered upper half."""
    zm = h * 0.50
    lo = cq.Workplane("XY").box(sx, sy, zm, centered=(True, True, False))
    hi = (cq.Workplane("XY").workplane(offset=zm).rect(sx, sy)
          .workplane(offset=h - zm).rect(sx - 2 * draft, sy - 2 * draft).loft())
    return lo.union(hi)


def leaded_ic(cx, cy, sx, sy, h, lead_len, lead_w, rows, **lead_kw):
    """rows: list of (direction, [positions along the side])."""
    body = ic_body(sx, sy, h)
    leads = []
    for d, positions in rows:
        for p in positions:
            lead = gullwing(lead_len, lead_w, h, **lead_kw)
            if d == "+Y":
                lead = lead.translate((p, sy / 2, 0))
            elif d == "-Y":
                lead = lead.rotate((0, 0, 0), (0, 0, 1), 180).translate((p, -sy / 2, 0))
            elif d == "+X":
                lead = lead.rotate((0, 0, 0), (0, 0, 1), -90).translate((sx / 2, p, 0))
            else:
                lead = lead.rotate((0, 0, 0), (0, 0, 1), 90).translate((-sx / 2, p, 0))
            leads.append(lead)
    return fuse_all(body, leads).translate((cx, cy, T))


def row(n, pitch):
    return [(i - (n - 1) / 2) * pitch for i in range(n)]


# U1 : leadless IC
U1_C = (-0.87, -0.04)
U1_S = (3.90, 5.30, 1.15)
u1 = box(U1_C[0] - U1_S[0] / 2, U1_C[0] + U1_S[0] / 2,
         U1_C[1] - U1_S[1] / 2, U1_C[1] + U1_S[1] / 2, T, T + U1_S[2])
u1 = u1.cut(cq.Workplane("XY").circle(0.07).extrude(0.1)
            .translate((U1_C[0] - U1_S[0] / 2 + 0.3, U1_C[1] - U1_S[1] / 2 + 0.3,
                        T + U1_S[2] - 0.05)))

# U2 : TSSOP-16, leads on +/-Y
U2_C = (3.99, -0.50)
U2_S = (4.96, 4.37, 1.10)
u2 = leaded_ic(U2_C[0], U2_C[1], U2_S[0], U2_S[1], U2_S[2], 1.05, 0.25,
               [("+Y", row(8, 0.65)), ("-Y", row(8, 0.65))])
u2 = u2.cut(cq.Workplane("XY").circle(0.40).extrude(0.2)
            .translate((2.25, -1.92, T + U2_S[2] - 0.05)))

# U3 : SOT-23-5 (3 leads on -Y, 2 on +Y)
U3_C = (5.14, -6.80)
u3 = leaded_ic(U3_C[0], U3_C[1], 2.90, 1.60, 1.07, 0.65, 0.40,
               [("-Y", row(3, 0.95)), ("+Y", [-0.95, 0.95])],
               t=0.14, exit_frac=0.55, foot=0.32, bend_r=0.2)

# U4 : SC70-6, leads on +/-X
U4_C = (-4.57, 8.87)
u4 = leaded_ic(U4_C[0], U4_C[1], 1.25, 2.00, 0.95, 0.47, 0.25,
               [("+X", row(3, 0.65)), ("-X", row(3, 0.65))],
               exit_frac=0.52, foot=0.25, bend_r=0.15)


u4 = u4.cut(cq.Workplane("XY").circle(0.08).extrude(0.1)
            .translate((U4_C[0] + 0.35, U4_C[1] - 0.7, T + 0.95 - 0.05)))


# ---------------------------------------------------------------
# resistor arrays (4 x 0603, castellated terminals)
# ---------------------------------------------------------------
def res_array(cx, cy, vertical):
    """4 x 0603 chip resistor array with castellated wrap-around terminals."""
    L, W, H = 3.20, 1.60, 0.50
    TERM_W, TERM_D, TERM_T = 0.50, 0.32, 0.03
    NOTCH_W, NOTCH_D = 0.26, 0.26
    b = box(-L / 2, L / 2, -W / 2, W / 2, 0, H)
    for i in range(4):
        x = (i - 1.5) * 0.8
        for s in (-1, 1):
            b = b.union(box(x - TERM_W / 2, x + TERM_W / 2, s * (W / 2 - TERM_D), s * W / 2,
                            H - 0.01, H + TERM_T))
            notch = (cq.Workplane("XY").center(x, s * W / 2)
                     .slot2D(2 * NOTCH_D, NOTCH_W, angle=90).extrude(H + 0.2)
                     .translate((0, 0, -0.1)))
            b = b.cut(notch)
    if vertical:
        b = b.rotate((0, 0, 0), (0, 0, 1), 90)
    return b.translate((cx, cy, T))


rn1 = res_array(-4.48, 5.50, True)
rn2 = res_array(-0.28, 5.21, False)
rn3 = res_array(-4.91, -6.66, True)


# ---------------------------------------------------------------
# passives
# ---------------------------------------------------------------
# 1206 style part (rounded vertical edges, grooved body)
P1206_C = (-4.91, -1.29)
c1206 = (cq.Workplane("XY").rect(1.60, 3.20).extrude(0.55)
         .edges("|Z").fillet(0.25)
         .translate((P1206_C[0], P1206_C[1], T)))
c1206 = c1206.union(cq.Workplane("XY").rect(1.54, 3.14).extrude(0.45)
                    .edges("|Z").fillet(0.22)
                    .translate((P1206_C[0], P1206_C[1], T + 0.55)))
c1206 = c1206.cut(box(P1206_C[0] - 1.0, P1206_C[0] + 1.0,
                      P1206_C[1] - 1.7, P1206_C[1] - 1.50, T + 0.15, T + 0.85))

caps = [
    # (cx, cy, sx, sy, h, fillet)
    (-4.43, 1.35, 1.65, 0.85, 0.80, 0.12),
    (-4.79, -3.99, 1.65, 0.85, 0.80, 0.12),
    (-5.24, 11.42, 1.65, 0.85, 0.80, 0.12),
    (-2.36, -5.22, 0.85, 1.65, 0.80, 0.12),
    (-1.04, -5.08, 0.85, 1.65, 0.80, 0.12),
    (1.57, -5.81, 2.05, 1.30, 0.85, 0.14),
    (4.84, -9.69, 2.05, 1.30, 0.85, 0.14),
]
cap_solids = [rbox(cx, cy, sx, sy, h, r) for (cx, cy, sx, sy, h, r) in caps]

# 0603 LED
LED_C = (-4.08, -11.18)
led = box(LED_C[0] - 0.42, LED_C[0] + 0.42, LED_C[1] - 0.80, LED_C[1] + 0.80, T, T + 0.75)
for s in (-1, 1):
    led = led.cut(box(LED_C[0] - 0.12, LED_C[0] + 0.12, LED_C[1] + s * 0.8 - 0.15,
                      LED_C[1] + s * 0.8 + 0.15, T - 0.1, T + 0.85))


# ---------------------------------------------------------------
# underside land pattern (shallow pad recesses around a rectangle)
# ---------------------------------------------------------------
BOT_C = (-0.02, -0.05)
BOT_S = (3.65, 5.20)
PAD_T = 0.03
bot_pads = None
nx, ny = 7, 10
for i in range(nx):
    x = BOT_C[0] + (i - (nx - 1) / 2) * (BOT_S[0] - 0.7) / (nx - 1)
    for s in (-1, 1):
        y = BOT_C[1] + s * (BOT_S[1] / 2 - 0.25)
        p = box(x - 0.12, x + 0.12, y - 0.25, y + 0.25, -0.1, PAD_T)
        bot_pads = p if bot_pads is None else bot_pads.union(p)
for j in range(ny):
    y = BOT_C[1] + (j - (ny - 1) / 2) * (BOT_S[1] - 1.1) / (ny - 1)
    for s in (-1, 1):
        x = BOT_C[0] + s * (BOT_S[0] / 2 - 0.25)
        p = box(x - 0.25, x + 0.25, y - 0.12, y + 0.12, -0.1, PAD_T)
        bot_pads = bot_pads.union(p)


# ---------------------------------------------------------------
# assemble
# ---------------------------------------------------------------
result = fuse_all(board.cut(bot_pads),
                  [j_front, j_back, u1, u2, u3, u4, rn1, rn2, rn3, c1206, led] + cap_solids)

VIEW = {"azimuth": 45, "elevation": 26}
